import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
W = 100.0          # plate width  (X)
D = 100.0          # plate depth  (Y), front edge at y=-D/2
H = 22.2           # overall height (leg foot to top face)
SKIN = 1.5         # top skin thickness over the underside pocket
Z_CEIL = H - SKIN  # ceiling of the underside pocket
Z_RIM = 15.1       # underside of front wall, bosses and rear hooks
Z_RAIL = 11.6      # underside of the side rails
R_FRONT = 6.8      # front vertical corner radius

LEG_W = 14.3       # leg width in X
LEG_D_A = 14.5     # foot depth of the outer strip
LEG_D_B = 17.7     # foot depth of the rail zone
LEG_CORE_D = 15.0  # depth of the inner part of the leg
LEG_CORE_R = 5.0   # rounding of the leg's inner rear corner
A_W = 3.1          # outer strip width (set back at the rear corners)
NOTCH_Y = 1.8      # set-back of the outer strip at the rear corners (top face)
RAIL_IN = 44.0     # |x| of the rail / pocket side wall (at the rim level)
FRONT_WALL = 3.8   # front wall thickness (at the rim level)
FRONT_EDGE_R = 1.2 # rounding of the lower front edge between the legs

LIP_OUT = 3.5      # hook protrusion beyond the rear edge
HOOK_R = 1.3       # plan rounding of the outer hook corners
HOOK_BOT_R = 1.2   # rounding of the hook's lower rear edge
TAB_L = (-W / 2 + A_W, 12.5)      # long rear hook x-range
TAB_S = (30.8, W / 2 - A_W)       # short rear hook x-range

HOLE_D = 7.7
CSK_D = 17.6
CBORE_D = 19.4
CBORE_DEPTH = 0.3
HOLES = [(-33.9, 16.9), (33.9, 16.9), (0.0, -35.6)]
BOSS_R = [10.5, 10.5, 10.8]   # boss radii at the rim level
POCKET_BLEND = 9.0     # plan radius of the S-blends between bosses and walls
POCKET_TAPER = 40.0    # draft of the pocket walls (deg from vertical)

FOOT_HOLE_D = 5.6
FOOT_HOLE_DEPTH = 10.0
FOOT_HOLE_X = 41.4
FOOT_HOLE_Y = -41.6

y0 = -D / 2
y1 = D / 2
c45 = math.cos(math.pi / 4)


def yz_prism(pts, xa, xb):
    """Extrude a closed (y, z) polygon between x = xa and x = xb."""
    return (cq.Workplane("YZ", origin=(xa, 0, 0)).polyline(pts).close()
            .extrude(xb - xa))


def box(x0_, x1_, ya, yb, za, zb):
    return (cq.Workplane("XY").box(x1_ - x0_, yb - ya, zb - za, centered=False)
            .translate((x0_, ya, za)))


# ---------------- plate slab (skin + underside solid down to the rim level) ----------------
body = box(-W / 2, W / 2, y0, y1, Z_RIM, H)

# ---------------- side structures (both sides) ----------------
for s in (1, -1):
    def xr(a, b):
        return (min(s * a, s * b), max(s * a, s * b))
    # outer strip: leg + 45 deg slant + rim, rear end cut back at 45 deg
    prof_a = [(y0, 0), (y0 + LEG_D_A, 0), (y0 + LEG_D_A + Z_RIM, Z_RIM),
              (y1 - NOTCH_Y - (H - Z_RIM), Z_RIM), (y1 - NOTCH_Y, H), (y0, H)]
    # rail zone: deeper foot, slant to rail underside, rail, slant up at rear
    prof_b = [(y0, 0), (y0 + LEG_D_B, 0), (y0 + LEG_D_B + Z_RAIL, Z_RAIL),
              (y1 - 7.5, Z_RAIL), (y1 - 7.5 + (Z_RIM - Z_RAIL), Z_RIM),
              (y1, Z_RIM), (y1, H), (y0, H)]
    body = body.union(yz_prism(prof_a, *xr(W / 2 - A_W, W / 2)))
    body = body.union(yz_prism(prof_b, *xr(RAIL_IN, W / 2 - A_W)))
    # rear corner of the outer strip cut back at 45 deg
    cut_a = [(y1 - NOTCH_Y - (H - Z_RIM) - 0.01, Z_RIM - 0.01), (y1 + 10, Z_RIM - 0.01), (y1 + 10, H + 1),
             (y1 - NOTCH_Y + 0.99, H + 1)]
    body = body.cut(yz_prism(cut_a, *xr(W / 2 - A_W, W / 2 + 1)))

# ---------------- rear hooks (dovetail tabs), added before the pocket is cut ----------------
def hook_prism(xa_, xb_):
    rb = HOOK_BOT_R
    return (cq.Workplane("YZ", origin=(xa_, 0, 0))
            .moveTo(y1 - 1.0, Z_RIM)
            .lineTo(y1 + LIP_OUT - rb, Z_RIM)
            .threePointArc((y1 + LIP_OUT - rb + rb * c45, Z_RIM + rb - rb * c45), (y1 + LIP_OUT, Z_RIM + rb))
            .lineTo(y1 + LIP_OUT, 17.2)
            .lineTo(y1 + 0.3, 20.4)
            .lineTo(y1, Z_CEIL)
            .lineTo(y1, H - 0.3)
            .lineTo(y1 - 1.0, H - 0.3)
            .close()
            .extrude(xb_ - xa_))


for (xa_, xb_), rounded in ((TAB_L, "<X"), (TAB_S, ">X")):
    hk = hook_prism(xa_, xb_)
    plan = (cq.Sketch().push([((xa_ + xb_) / 2, y1 + LIP_OUT - 4.75)])
            .rect(xb_ - xa_, 9.5).reset()
            .vertices(">Y and " + rounded).fillet(HOOK_R))
    hk = hk.intersect(cq.Workplane("XY").placeSketch(plan).extrude(H))
    body = body.union(hk)

# ---------------- central underside pocket (sloped walls, S-blends around the bosses) ----------------
pk_y0 = y0 + FRONT_WALL
pk_y1 = y1 + 0.1          # pocket reaches the inner face of the hooks
pocket_sk = (cq.Sketch()
             .push([(0, (pk_y0 + pk_y1) / 2)])
             .rect(2 * RAIL_IN, pk_y1 - pk_y0)
             .reset())
for (hx, hy), r in zip(HOLES, BOSS_R):
    pocket_sk = pocket_sk.push([(hx, hy)]).circle(r, mode="s").reset()
# round every salient corner of the pocket outline (S-blends): erode, then dilate
pk_wire = pocket_sk.faces().vals()[0].outerWire()
pk_wire = pk_wire.offset2D(-POCKET_BLEND, "arc")[0].offset2D(POCKET_BLEND, "arc")[0]
pk_face = cq.Face.makeFromWires(pk_wire)
# straight part below the rim level, then walls sloping in up to the ceiling
pk_low = cq.Solid.extrudeLinear(pk_face, cq.Vector(0, 0, Z_RIM + 1.0)).translate(cq.Vector(0, 0, -1.0))
pk_up = cq.Solid.extrudeLinear(pk_face, cq.Vector(0, 0, Z_CEIL - Z_RIM), taper=POCKET_TAPER)
pk_up = pk_up.translate(cq.Vector(0, 0, Z_RIM))
body = body.cut(cq.Workplane("XY").add(pk_low)).cut(cq.Workplane("XY").add(pk_up))
# gap between the two hooks: the pocket runs out through the rear edge
body = body.cut(box(TAB_L[1], TAB_S[0], y1 - 7.0, y1 + 10, -1.0, Z_CEIL))

# ---------------- legs (inner core, rounded rear corner) ----------------
for s in (1, -1):
    core_sk = (cq.Sketch()
               .push([(s * (W / 2 - LEG_W + (LEG_W - A_W) / 2), y0 + LEG_CORE_D / 2)])
               .rect(LEG_W - A_W, LEG_CORE_D)
               .reset()
               .vertices(">Y and " + ("<X" if s > 0 else ">X"))
               .fillet(LEG_CORE_R))
    core = cq.Workplane("XY").placeSketch(core_sk).extrude(H)
    body = body.union(core)

# ---------------- outline: round front corners ----------------
outline = (cq.Workplane("XY")
           .moveTo(-W / 2 + R_FRONT, y0)
           .lineTo(W / 2 - R_FRONT, y0)
           .threePointArc((W / 2 - R_FRONT + R_FRONT * c45, y0 + R_FRONT - R_FRONT * c45),
                          (W / 2, y0 + R_FRONT))
           .lineTo(W / 2, y1 + LIP_OUT + 1)
           .lineTo(-W / 2, y1 + LIP_OUT + 1)
           .lineTo(-W / 2, y0 + R_FRONT)
           .threePointArc((-W / 2 + R_FRONT - R_FRONT * c45, y0 + R_FRONT - R_FRONT * c45),
                          (-W / 2 + R_FRONT, y0))
           .close()
           .extrude(H))
body = body.intersect(outline)

# ---------------- rounded lower front edge of the front wall (between the legs) ----------------
fr = FRONT_EDGE_R
edge_cut = (cq.Workplane("YZ", origin=(-(W / 2 - LEG_W), 0, 0))
            .moveTo(y0 - 1.0, Z_RIM - 1.0).lineTo(y0 + fr, Z_RIM - 1.0).lineTo(y0 + fr, Z_RIM)
            .threePointArc((y0 + fr - fr * c45, Z_RIM + fr - fr * c45), (y0, Z_RIM + fr))
            .lineTo(y0 - 1.0, Z_RIM + fr).close()
            .extrude(2 * (W / 2 - LEG_W)))
body = body.cut(edge_cut)

# ---------------- holes: through bore, countersink + counterbore from below ----------------
for (hx, hy) in HOLES:
    body = body.cut(cq.Workplane("XY").center(hx, hy).circle(HOLE_D / 2).extrude(H + 1))
    csk_h = (CSK_D - HOLE_D) / 2.0
    cone = cq.Solid.makeCone(CSK_D / 2, HOLE_D / 2, csk_h,
                             pnt=cq.Vector(hx, hy, Z_RIM + CBORE_DEPTH), dir=cq.Vector(0, 0, 1))
    body = body.cut(cq.Workplane("XY").add(cone))
    body = body.cut(cq.Workplane("XY").center(hx, hy).circle(CBORE_D / 2)
                    .extrude(Z_RIM + CBORE_DEPTH + 1).translate((0, 0, -1)))

# ---------------- blind holes in the leg feet ----------------
for s in (1, -1):
    fx = s * FOOT_HOLE_X
    body = body.cut(cq.Workplane("XY").center(fx, FOOT_HOLE_Y).circle(FOOT_HOLE_D / 2)
                    .extrude(FOOT_HOLE_DEPTH + 1).translate((0, 0, -1)))

result = body
